import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_X = 80.0        # plate width (X)
PLATE_Y = 101.6       # plate depth (Y)
PLATE_T = 1.7         # plate thickness
HEIGHT = 15.3         # overall height (top of corner posts)
CORNER_R = 3.0        # outer vertical corner radius (plate and posts)

POST_X = 13.1         # post extent along X from the outer edge
POST_Y = 14.0         # post extent along Y from the outer edge
CHAMFER_SUM = 16.0    # inner chamfer line: u + v = CHAMFER_SUM (corner-local)
POST_EDGE_R = 1.0     # rounding of the post's inner vertical edges (chamfer ends)
JUNCTION_R = 0.6      # rounding where the post inner sides meet the outer walls

BASE_FILLET = 6.2     # fillet radius at the foot of the posts
FILLET_INSET = 0.25   # fillet was made on a post this much smaller; the
                      # post walls were then pushed out, so the fillet meets
                      # the wall with a slight crease

HOLE_D = 3.2          # blind hole diameter in post tops
HOLE_DEPTH = 8.0
HOLE_U = 4.4          # hole centre from the X-side edge
HOLE_V = 5.3          # hole centre from the Y-side edge

VIEW = {"azimuth": 45, "elevation": 26}

hx, hy = PLATE_X / 2.0, PLATE_Y / 2.0
EPS = 1e-3
CORNERS = [(1, 1), (-1, 1), (-1, -1), (1, -1)]


class EdgeFilter(cq.Selector):
    """Select edges satisfying a predicate."""

    def __init__(self, pred):
        self.pred = pred

    def filter(self, objectList):
        return [o for o in objectList if self.pred(o)]


def is_vertical(e):
    p0, p1 = e.startPoint(), e.endPoint()
    return abs(p0.x - p1.x) < EPS and abs(p0.y - p1.y) < EPS and abs(p0.z - p1.z) > EPS


def near_any(c, pts):
    return any(abs(c.x - px) < EPS and abs(c.y - py) < EPS for px, py in pts)


def to_global(sx, sy, u, v):
    """corner-local (u inward from the X wall, v inward from the Y wall) -> global XY"""
    return (sx * (hx - u), sy * (hy - v))


def post_local(inset):
    """Post footprint in corner-local coordinates; the inner sides are moved
    inward by `inset` (outer sides stay on the plate boundary)."""
    sx_, sy_ = POST_X - inset, POST_Y - inset
    c = CHAMFER_SUM - inset * math.sqrt(2.0)
    return [(0.0, 0.0), (sx_, 0.0), (sx_, c - sx_), (c - sy_, sy_), (0.0, sy_)]


def rounded_polygon(pts, radii, z0, height):
    """Extrude a closed polygon whose vertices are rounded with the given radii."""
    n = len(pts)
    segs = []
    for i in range(n):
        p = pts[i]
        a = pts[i - 1]
        b = pts[(i + 1) % n]
        r = radii[i]
        d1 = (p[0] - a[0], p[1] - a[1])
        l1 = math.hypot(*d1)
        d1 = (d1[0] / l1, d1[1] / l1)
        d2 = (b[0] - p[0], b[1] - p[1])
        l2 = math.hypot(*d2)
        d2 = (d2[0] / l2, d2[1] / l2)
        if r <= 0:
            segs.append((p, None, p))
            continue
        cosang = -(d1[0] * d2[0] + d1[1] * d2[1])
        theta = math.acos(max(-1.0, min(1.0, cosang)))        # interior angle
        t = r / math.tan(theta / 2.0)
        t1 = (p[0] - d1[0] * t, p[1] - d1[1] * t)
        t2 = (p[0] + d2[0] * t, p[1] + d2[1] * t)
        bis = (-d1[0] + d2[0], -d1[1] + d2[1])
        lb = math.hypot(*bis)
        bis = (bis[0] / lb, bis[1] / lb)
        dc = r / math.sin(theta / 2.0)
        cen = (p[0] + bis[0] * dc, p[1] + bis[1] * dc)
        mid = (cen[0] - bis[0] * r, cen[1] - bis[1] * r)
        segs.append((t1, mid, t2))
    wp = cq.Workplane("XY").workplane(offset=z0).moveTo(*segs[0][2])
    for i in range(1, n + 1):
        t1, mid, t2 = segs[i % n]
        wp = wp.lineTo(*t1)
        if mid is not None:
            wp = wp.threePointArc(mid, t2)
    return wp.close().extrude(height)


# ---------------- plate + (slightly smaller) posts ----------------
body = cq.Workplane("XY").box(PLATE_X, PLATE_Y, PLATE_T, centered=(True, True, False))
small = post_local(FILLET_INSET)
for sx, sy in CORNERS:
    pts = [to_global(sx, sy, u, v) for u, v in small]
    body = body.union(cq.Workplane("XY").polyline(pts).close().extrude(HEIGHT))

# outer vertical corners (full height)
body = body.edges(EdgeFilter(lambda e: is_vertical(e)
                             and abs(abs(e.Center().x) - hx) < EPS
                             and abs(abs(e.Center().y) - hy) < EPS)).fillet(CORNER_R)

# inner vertical edges at both ends of the chamfer
inner_pts = []
for sx, sy in CORNERS:
    inner_pts.append(to_global(sx, sy, *small[2]))
    inner_pts.append(to_global(sx, sy, *small[3]))
body = body.edges(EdgeFilter(lambda e: is_vertical(e) and near_any(e.Center(), inner_pts))
                  ).fillet(POST_EDGE_R - FILLET_INSET)


# fillet at the foot of the posts (runs out at the outer walls)
def is_base_edge(e):
    bb = e.BoundingBox()
    if abs(bb.zmin - PLATE_T) > EPS or bb.zlen > EPS:
        return False
    c = e.Center()
    return abs(c.x) < hx - EPS and abs(c.y) < hy - EPS


body = body.edges(EdgeFilter(is_base_edge)).fillet(BASE_FILLET)

# ---------------- full-size posts (walls pushed out) ----------------
full = post_local(0.0)
radii = [CORNER_R, 0.0, POST_EDGE_R, POST_EDGE_R, 0.0]
for sx, sy in CORNERS:
    pts = [to_global(sx, sy, u, v) for u, v in full]
    body = body.union(rounded_polygon(pts, radii, PLATE_T, HEIGHT - PLATE_T))

# height above the plate where the foot fillet meets the pushed-out wall
MEET_H = BASE_FILLET - math.sqrt(2.0 * BASE_FILLET * FILLET_INSET - FILLET_INSET ** 2)

# round the vertical edges where the post inner sides meet the outer walls,
# from the top of the foot fillet up to the post top
# (cutter = small corner square minus a quarter cylinder)
z0 = PLATE_T + MEET_H
zlen = HEIGHT - z0 + 1.0
r = JUNCTION_R
for sx, sy in CORNERS:
    for (u, v) in ((POST_X, 0.0), (0.0, POST_Y)):
        jx, jy = to_global(sx, sy, u, v)
        if v == 0.0:   # X-facing inner side meets the Y outer wall
            ax, ay = (sx * 1.0, 0.0), (0.0, -sy * 1.0)
        else:          # Y-facing inner side meets the X outer wall
            ax, ay = (0.0, sy * 1.0), (-sx * 1.0, 0.0)
        p0 = (jx, jy)
        p1 = (jx + ax[0] * r, jy + ax[1] * r)
        p2 = (jx + (ax[0] + ay[0]) * r, jy + (ax[1] + ay[1]) * r)
        p3 = (jx + ay[0] * r, jy + ay[1] * r)
        square = (cq.Workplane("XY").workplane(offset=z0)
                  .polyline([p0, p1, p2, p3]).close().extrude(zlen))
        cyl = (cq.Workplane("XY").workplane(offset=z0 - 0.5)
               .center(p2[0], p2[1]).circle(r).extrude(zlen + 1.0))
        body = body.cut(square.cut(cyl))

# ---------------- blind holes in post tops ----------------
hole_pts = [to_global(sx, sy, HOLE_U, HOLE_V) for sx, sy in CORNERS]
body = (body.faces(">Z").workplane(origin=(0, 0, HEIGHT))
        .pushPoints(hole_pts).hole(HOLE_D, HOLE_DEPTH))

result = body
